import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# loop handle (stadium-shaped ring standing in the XZ plane)
ring_len = 81.5          # overall outer length along X
ring_h = 30.4            # overall outer height along Z
ring_bar = 6.9           # bar width in the ring plane
ring_thk = 12.7          # ring thickness along Y

# stem joining ring and flange (stadium section in XY)
stem_len = 23.5
stem_w = 9.0

# flange / washer head
flange_d = 40.0
flange_t = 3.2
flange_fillet = 2.3

# collar under the flange
collar_d = 25.5
collar_h = 3.0

# coarse helical thread: sawtooth tooth with a slightly sloped underside,
# a short cylindrical crest land and a conical upper flank
thread_len = 11.15
thread_crest_d = 23.2
thread_root_d = 13.8
thread_pitch = 7.2
tooth_under = 0.8        # axial rise of the underside from root to crest
tooth_land = 1.2         # axial length of the cylindrical crest land
tooth_flank = 5.0        # axial height of the upper conical flank (crest -> root)
thread_phase = 0.6       # height of the tooth root-bottom above the shank tip, at +X

# vertical layout (flange underside at z = 0)
stem_z0 = flange_t
ring_bottom_z = 13.4
ring_cz = ring_bottom_z + ring_h / 2.0

# ---------------- ring ----------------
# stadium-section bar (full round toward +/-Y) swept around a stadium centreline
path_r = (ring_h - ring_bar) / 2.0            # centreline radius of the end bends
path_a = (ring_len - ring_h) / 2.0            # half length of the straight bars
path = (
    cq.Workplane("XZ")
    .moveTo(0, ring_cz - path_r)
    .lineTo(path_a, ring_cz - path_r)
    .threePointArc((path_a + path_r, ring_cz), (path_a, ring_cz + path_r))
    .lineTo(-path_a, ring_cz + path_r)
    .threePointArc((-path_a - path_r, ring_cz), (-path_a, ring_cz - path_r))
    .close()
)
ring = (
    cq.Workplane("YZ", origin=(0, 0, ring_cz - path_r))
    .slot2D(ring_thk, ring_bar)
    .sweep(path)
)

# ---------------- stem ----------------
stem = (
    cq.Workplane("XY", origin=(0, 0, stem_z0 - 0.5))
    .slot2D(stem_len, stem_w)
    .extrude(ring_bottom_z + ring_bar / 2.0 - stem_z0 + 0.5)
)

# ---------------- flange ----------------
flange = (
    cq.Workplane("XY")
    .circle(flange_d / 2.0)
    .extrude(flange_t)
    .faces(">Z").edges()
    .fillet(flange_fillet)
)

# ---------------- collar ----------------
collar = (
    cq.Workplane("XY", origin=(0, 0, -collar_h))
    .circle(collar_d / 2.0)
    .extrude(collar_h + 0.5)
)

# ---------------- threaded shank ----------------
z_bot = -collar_h - thread_len
r_root = thread_root_d / 2.0
r_crest = thread_crest_d / 2.0
core = (
    cq.Workplane("XY", origin=(0, 0, z_bot))
    .circle(r_root)
    .extrude(thread_len + 0.5)
)

z_start = z_bot + thread_phase - 2 * thread_pitch
helix_h = thread_len + 3 * thread_pitch
helix = cq.Wire.makeHelix(thread_pitch, helix_h, r_root, center=cq.Vector(0, 0, z_start))
flank_slope = tooth_flank / (r_crest - r_root)
under_slope = tooth_under / (r_crest - r_root)
r_in = r_root - 0.1      # tooth root sunk slightly into the core for a clean union
tooth = (
    cq.Workplane("XZ", origin=(0, 0, 0))
    .polyline([
        (r_in, z_start - 0.1 * under_slope),
        (r_crest, z_start + tooth_under),
        (r_crest, z_start + tooth_under + tooth_land),
        (r_in, z_start + tooth_under + tooth_land + tooth_flank + 0.1 * flank_slope),
    ])
    .close()
    .sweep(cq.Workplane("XY").add(helix), isFrenet=True)
)
trim = (
    cq.Workplane("XY", origin=(0, 0, z_bot))
    .circle(r_crest + 1.0)
    .extrude(thread_len)
)
shank = core.union(tooth.intersect(trim))

result = (
    ring.union(stem)
    .union(flange)
    .union(collar)
    .union(shank)
)

VIEW = {"azimuth": 45, "elevation": 26}
